import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# Axisymmetric stepped bushing / grommet, axis = Z, bottom face at Z=0.
R_FLANGE = 29.55     # central flange radius
R_BODY = 24.95       # upper / lower body radius
R_NECK = 19.68       # top neck and bottom spigot radius
CHAMF = 2.7          # 45 deg chamfer on the top outer edge of the neck

H_NECK = 5.4         # height of top neck and of bottom spigot
H_BODY = 7.68        # height of upper and of lower body
H_FLANGE = 10.6      # flange thickness

F_BODY = 2.45        # outer edge fillets (body shoulders, spigot bottom)

R_BORE = 10.0        # central counterbore radius (open at the top)
F_BORE_TOP = 2.7     # round on the bore mouth
F_BORE_BOT = 3.4     # round at the bore floor
BORE_FLOOR = 8.0     # height of the bore floor above the bottom face
R_HOLE = 3.35        # small through hole in the bore floor

# The part is fully axisymmetric; these angles only place the (invisible in
# reality) seam lines of the periodic faces away from the main viewing side.
SEAM_OUT = 135.0
SEAM_IN = 45.0

# ---------------- derived levels ----------------
Z1 = H_NECK                  # spigot top / lower body bottom
Z2 = Z1 + H_BODY             # flange bottom
Z3 = Z2 + H_FLANGE           # flange top
Z4 = Z3 + H_BODY             # upper body top / neck bottom
Z5 = Z4 + H_NECK             # overall top


def cyl(r, z0, z1, rot=0.0):
    c = cq.Workplane("XY").workplane(offset=z0).circle(r).extrude(z1 - z0)
    return c.rotate((0, 0, 0), (0, 0, 1), rot) if rot else c


class CircleAt(cq.Selector):
    """Select circular edges lying in plane Z=z with radius r."""

    def __init__(self, z, r, tol=0.05):
        self.z, self.r, self.tol = z, r, tol

    def filter(self, objs):
        out = []
        for e in objs:
            bb = e.BoundingBox()
            rad = max(abs(bb.xmin), abs(bb.xmax), abs(bb.ymin), abs(bb.ymax))
            if (abs(bb.zmin - self.z) < self.tol and abs(bb.zmax - self.z) < self.tol
                    and abs(rad - self.r) < self.tol):
                out.append(e)
        return out


# ---------------- outer stepped body ----------------
body = (
    cyl(R_NECK, 0, Z1)
    .union(cyl(R_BODY, Z1, Z2))
    .union(cyl(R_FLANGE, Z2, Z3))
    .union(cyl(R_BODY, Z3, Z4))
    .union(cyl(R_NECK, Z4, Z5))
)

body = body.edges(CircleAt(0, R_NECK)).fillet(F_BODY)      # spigot bottom
body = body.edges(CircleAt(Z1, R_BODY)).fillet(F_BODY)     # lower body shoulder
body = body.edges(CircleAt(Z4, R_BODY)).fillet(F_BODY)     # upper body shoulder
body = body.edges(CircleAt(Z5, R_NECK)).chamfer(CHAMF)     # neck top chamfer
body = body.rotate((0, 0, 0), (0, 0, 1), SEAM_OUT)

# ---------------- central counterbore + through hole ----------------
body = body.cut(cyl(R_BORE, BORE_FLOOR, Z5 + 1, SEAM_IN))
body = body.edges(CircleAt(Z5, R_BORE)).fillet(F_BORE_TOP)
body = body.edges(CircleAt(BORE_FLOOR, R_BORE)).fillet(F_BORE_BOT)
body = body.cut(cyl(R_HOLE, -1, BORE_FLOOR + 1, SEAM_IN))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
